import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0            # overall square size
H = W / 2.0
R_DISC = 50.0        # radius of the central disc
PAD = 25.0           # corner pad size (along each edge)
T = 8.0              # total thickness (pads)
STEP = 1.5           # pads protrude this much below the disc
RC = 4.5             # outer vertical corner radius of pads
RN = 3.0             # concave fillet where pad side meets disc
RF = 1.6             # top edge fillet

HOLE_D = 5.3         # corner mounting holes
HOLE_OFF = 11.7      # hole centre distance from outer edges

BOSS_D = 12.0        # central raised boss
BOSS_H = 1.1
BOSS_CH = 0.2        # chamfer on boss top edge
BORE_D = 7.3         # counterbore in boss
BORE_CH = 0.0        # chamfer at bore mouth
BORE_DEPTH = 3.0
THRU_D = 4.2         # central through hole
HUB_D = 8.0          # spline-hub recess on the underside
HUB_DEPTH = 1.5

SCREW_HEAD_D = 6.6   # countersunk screw heads (flush)
SCREW_D = 2.8
CROSS_L = 3.0        # cross recess in screw heads
CROSS_W = 0.8
CROSS_C = 1.4        # central cone/pocket of the cross recess
CROSS_DEPTH = 1.2
SCREW_POS = [(0, 11.0), (0, 21.0), (0, -11.0), (0, -21.0), (11.0, 0), (-11.0, 0)]

HORN_W = 8.0         # servo horn pocket on underside
HORN_LONG = 25.3     # centre of long-arm end radius (along Y)
HORN_SHORT = 10.8    # centre of short-arm end radius (along X)
HORN_DEPTH = 0.9
HORN_HOLE_D = 1.0    # small horn holes beside each screw
HORN_HOLE_OFF = 3.0

VIEW = {"azimuth": 45, "elevation": 26}


def _is_vertical(e):
    p0 = e.startPoint()
    p1 = e.endPoint()
    return abs(p0.x - p1.x) < 1e-6 and abs(p0.y - p1.y) < 1e-6 and abs(p0.z - p1.z) > 1e-3


# ---------------- main plate ----------------
disc = cq.Workplane("XY").circle(R_DISC).extrude(T)
pad_c = H - PAD / 2.0
pads = (
    cq.Workplane("XY")
    .pushPoints([(sx * pad_c, sy * pad_c) for sx in (-1, 1) for sy in (-1, 1)])
    .rect(PAD, PAD)
    .extrude(T)
)
body = disc.union(pads).val()

# round the outer vertical corners of the pads
corner_edges = []
for e in body.Edges():
    if _is_vertical(e):
        p = e.startPoint()
        if abs(abs(p.x) - H) < 1e-3 and abs(abs(p.y) - H) < 1e-3:
            corner_edges.append(e)
body = body.fillet(RC, corner_edges)

# concave fillets where pad sides meet the disc rim
yn = math.sqrt(R_DISC ** 2 - (H - PAD) ** 2)
notch_edges = []
for e in body.Edges():
    if _is_vertical(e):
        p = e.startPoint()
        ax, ay = abs(p.x), abs(p.y)
        if (abs(ax - (H - PAD)) < 1e-3 and abs(ay - yn) < 1e-3) or (
            abs(ay - (H - PAD)) < 1e-3 and abs(ax - yn) < 1e-3
        ):
            notch_edges.append(e)
body = body.fillet(RN, notch_edges)

# underside relief: disc area is thinner than the pads
relief = cq.Workplane("XY").rect(3 * W, 3 * W).extrude(STEP)
relief = relief.cut(
    cq.Workplane("XY")
    .pushPoints([(sx * pad_c, sy * pad_c) for sx in (-1, 1) for sy in (-1, 1)])
    .rect(PAD, PAD)
    .extrude(STEP)
)
body = body.cut(relief.val())

# fillet the top outer edges
top_edges = []
for e in body.Edges():
    p0, p1 = e.startPoint(), e.endPoint()
    if abs(p0.z - T) < 1e-6 and abs(p1.z - T) < 1e-6:
        top_edges.append(e)
body = body.fillet(RF, top_edges)

plate = cq.Workplane("XY").add(body)

# ---------------- corner holes ----------------
hc = H - HOLE_OFF
plate = plate.cut(
    cq.Workplane("XY")
    .pushPoints([(sx * hc, sy * hc) for sx in (-1, 1) for sy in (-1, 1)])
    .circle(HOLE_D / 2)
    .extrude(T)
)

# ---------------- central boss with bore ----------------
boss = (
    cq.Workplane("XY").workplane(offset=T)
    .circle(BOSS_D / 2).extrude(BOSS_H)
    .faces(">Z").edges().chamfer(BOSS_CH)
)
plate = plate.union(boss)
bore = (
    cq.Workplane("XY").workplane(offset=T + BOSS_H - BORE_DEPTH)
    .circle(BORE_D / 2).extrude(BORE_DEPTH)
)
if BORE_CH > 0:
    bore = bore.union(
        cq.Workplane("XY").workplane(offset=T + BOSS_H - BORE_CH)
        .circle(BORE_D / 2).workplane(offset=BORE_CH).circle(BORE_D / 2 + BORE_CH).loft()
    )
plate = plate.cut(bore)
plate = plate.cut(cq.Workplane("XY").circle(THRU_D / 2).extrude(T + BOSS_H))

# ---------------- underside servo-horn pocket ----------------
horn_h = STEP + HORN_DEPTH
horn = (
    cq.Workplane("XY")
    .slot2D(2 * HORN_LONG + HORN_W, HORN_W, angle=90)
    .extrude(horn_h)
    .union(cq.Workplane("XY").slot2D(2 * HORN_SHORT + HORN_W, HORN_W, angle=0).extrude(horn_h))
)
plate = plate.cut(horn)
# spline hub recess at the centre of the horn pocket
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=horn_h).circle(HUB_D / 2).extrude(HUB_DEPTH)
)
# small horn holes next to each screw (blind, in pocket floor)
small = []
for (x, y) in SCREW_POS:
    if x == 0:
        small += [(0, y - HORN_HOLE_OFF), (0, y + HORN_HOLE_OFF)]
    else:
        small += [(x - HORN_HOLE_OFF, 0), (x + HORN_HOLE_OFF, 0)]
small = [p for p in small if math.hypot(*p) > HUB_D / 2 + 1.0]
plate = plate.cut(
    cq.Workplane("XY").workplane(offset=horn_h)
    .pushPoints(small).circle(HORN_HOLE_D / 2).extrude(1.5)
)

# ---------------- flush countersunk screws (head outline + cross recess) ----------------
for (x, y) in SCREW_POS:
    # thin ring marking the head outline
    ring = (
        cq.Workplane("XY").workplane(offset=T - 0.3)
        .center(x, y)
        .circle(SCREW_HEAD_D / 2)
        .circle(SCREW_HEAD_D / 2 - 0.25)
        .extrude(0.3)
    )
    plate = plate.cut(ring)
    # cross recess
    cross = (
        cq.Workplane("XY").workplane(offset=T - CROSS_DEPTH)
        .center(x, y)
        .rect(CROSS_L, CROSS_W)
        .extrude(CROSS_DEPTH)
        .union(
            cq.Workplane("XY").workplane(offset=T - CROSS_DEPTH)
            .center(x, y).rect(CROSS_W, CROSS_L).extrude(CROSS_DEPTH)
        )
        .union(
            cq.Workplane("XY").workplane(offset=T - CROSS_DEPTH)
            .center(x, y).circle(CROSS_C / 2).extrude(CROSS_DEPTH)
        )
    )
    plate = plate.cut(cross)
    # screw clearance hole from the pocket floor up to the recess
    plate = plate.cut(
        cq.Workplane("XY").center(x, y).circle(SCREW_D / 2).extrude(T - CROSS_DEPTH)
    )

result = plate
